import math
import cadquery as cq
from cadquery import Vector

# =====================================================================
#  4-way tube connector: one axial spigot (-Y) plus three radial spigots
#  at 120 deg around it, each leaning TILT deg toward the axial one.
#  Concave gusset webs join the axial spigot to every radial spigot.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
D = 25.0              # spigot outer diameter
R = D / 2.0
BORE_D = 14.0         # spigot bore diameter
r = BORE_D / 2.0
L = 83.0              # spigot length, node centre -> spigot mouth
TILT = 14.5           # lean of the radial spigots toward the axial one (deg)
CAP_C = 11.5          # radial spigots begin this far from the node with a domed end
AX_CAP_C = 11.5       # same for the axial spigot (hidden inside the node)
END_ROUND = 2.7       # full round of the spigot mouth (outer and inner)
WEB_T = 6.4           # gusset web thickness
WEB_S = L - 3.0       # where the concave web edge runs into the spigots
WEB_ARC_K = 1.04      # concave edge radius relative to the fully tangent arc
FLARE_R = 14.0        # max radius of the node flare
FLARE_Y1 = 5.0        # ... reached this far down the axial spigot
FLARE_TOP = 3.0       # flare closes on the axis here (behind node centre)
HOLE_D = 5.0          # small through hole along the axial spigot
BORE_STOP_AX = 10.0   # axial bore floor, distance from node centre
BORE_STOP_RAD = 12.5  # radial bore floor, distance from node centre
DIMPLE_R = 4.5        # spherical dimples on the back of the radial spigots
DIMPLE_A = 16.0       # dimple position along the spigot from node centre
DIMPLE_OUT = 2.0      # dimple sphere centre lies this far outside the surface

VIEW = {"azimuth": 45, "elevation": 26}

th = math.radians(TILT)
AX = Vector(0, -1, 0)                              # axial spigot direction
# the node flare starts where axial spigot, radial spigot and web face meet
_xw = math.sqrt(R * R - (WEB_T / 2.0) ** 2)
FLARE_Y0 = _xw * math.cos(th) / (1.0 - math.sin(th))
K = 1.0 - math.sqrt(0.5)                           # quarter-arc mid point factor


def rot_y(v, deg):
    a = math.radians(deg)
    c, s = math.cos(a), math.sin(a)
    return Vector(v.x * c + v.z * s, v.y, -v.x * s + v.z * c)


U0 = Vector(math.cos(th), -math.sin(th), 0)        # radial spigot along +X
N0 = Vector(math.sin(th), math.cos(th), 0)         # its back-facing normal
ANGLES = [0.0, -120.0, 120.0]                      # +X, upper-left, lower-left
DIRS = [rot_y(U0, a) for a in ANGLES]
BACKN = [rot_y(N0, a) for a in ANGLES]


def axis_plane(u, seam):
    """plane with local x along u and local y toward 'seam' (revolve seam)"""
    w = (seam - u * seam.dot(u)).normalized()
    return cq.Plane(origin=(0, 0, 0), xDir=u, normal=u.cross(w))


def spigot(u, seam, cap_c):
    """solid spigot: domed inner end at cap_c, rounded mouth at L"""
    f = END_ROUND
    prof = (cq.Workplane(axis_plane(u, seam))
            .moveTo(cap_c - R, 0)
            .threePointArc((cap_c - R * math.sqrt(0.5), R * math.sqrt(0.5)), (cap_c, R))
            .lineTo(L - f, R)
            .threePointArc((L - f * K, R - f * K), (L, R - f))
            .lineTo(L, 0)
            .close())
    return prof.revolve(360, (0, 0, 0), (1, 0, 0))


def bore_tool(u, seam, stop):
    """bore from the mouth down to 'stop', with a rounded mouth edge"""
    f = END_ROUND
    prof = (cq.Workplane(axis_plane(u, seam))
            .moveTo(stop, 0)
            .lineTo(stop, r)
            .lineTo(L - f, r)
            .threePointArc((L - f * K, r + f * K), (L, r + f))
            .lineTo(L + 2.0, r + f)
            .lineTo(L + 2.0, 0)
            .close())
    return prof.revolve(360, (0, 0, 0), (1, 0, 0))


def seam_for(u):
    # put revolve seams inside the web joining u to the axial spigot
    return AX if abs(u.dot(AX)) < 0.99 else Vector(1, 0, 0)


# ---------------- spigots ----------------
body = spigot(AX, seam_for(AX), AX_CAP_C)
for u in DIRS:
    body = body.union(spigot(u, seam_for(u), CAP_C))

# ---------------- node flare around the axial spigot ----------------
flare = (cq.Workplane("XY")
         .polyline([(0, -FLARE_Y0), (R, -FLARE_Y0), (FLARE_R, -FLARE_Y1), (0, FLARE_TOP)])
         .close()
         .revolve(360, (0, 0, 0), (0, 1, 0)))
body = body.union(flare)


# ---------------- concave gusset webs ----------------
def make_web(u):
    e1 = AX
    e2 = (u - e1 * u.dot(e1)).normalized()
    nrm = e1.cross(e2)
    ux, uy = u.dot(e1), u.dot(e2)                    # u in local (e1, e2) coords
    half = math.acos(max(-1.0, min(1.0, ux))) / 2.0  # half angle between spigots
    rho = WEB_S * math.tan(half) - R                 # radius of the concave edge
    t1 = (WEB_S, R)                                  # tangent point, axial spigot
    nux, nuy = uy, -ux
    if nux < 0:
        nux, nuy = -nux, -nuy
    t2 = (WEB_S * ux + R * nux, WEB_S * uy + R * nuy)  # tangent point, radial spigot
    bx, by = 1 + ux, uy
    bl = math.hypot(bx, by)
    bx, by = bx / bl, by / bl
    # arc through t1 and t2, centre on the bisector, radius WEB_ARC_K * rho
    half_chord = math.hypot(t2[0] - t1[0], t2[1] - t1[1]) / 2.0
    rho_k = max(rho * WEB_ARC_K, half_chord + 1e-3)
    cmid = ((t1[0] + t2[0]) / 2.0, (t1[1] + t2[1]) / 2.0)
    cdist = math.hypot(*cmid) + math.sqrt(rho_k ** 2 - half_chord ** 2)
    mx, my = bx * (cdist - rho_k), by * (cdist - rho_k)  # arc mid point
    a1 = (WEB_S, 0.0)
    a2 = (WEB_S * ux, WEB_S * uy)
    pl = cq.Plane(origin=(0, 0, 0), xDir=e1, normal=nrm)
    return (cq.Workplane(pl)
            .moveTo(0, 0).lineTo(*a1).lineTo(*t1)
            .threePointArc((mx, my), t2)
            .lineTo(*a2).close()
            .extrude(WEB_T / 2.0, both=True))


for u in DIRS:
    body = body.union(make_web(u))

# ---------------- bores, through hole, dimples ----------------
cut = bore_tool(AX, seam_for(AX), BORE_STOP_AX)
for u in DIRS:
    cut = cut.union(bore_tool(u, seam_for(u), BORE_STOP_RAD))
cut = cut.union(cq.Workplane("XY").add(
    cq.Solid.makeCylinder(HOLE_D / 2.0, L + R + 5.0, Vector(0, -L, 0), Vector(0, 1, 0))))
for u, n in zip(DIRS, BACKN):
    c = u * DIMPLE_A + n * (R + DIMPLE_OUT)
    cut = cut.union(cq.Workplane("XY").add(cq.Solid.makeSphere(DIMPLE_R, pnt=c)))

body = body.cut(cut)

result = body
